import math
import cadquery as cq
from cadquery.occ_impl.shapes import BRepFilletAPI_MakeFillet

# ============ NEMA-style motor corner bracket ============
# Front plate (normal -Y) carries the motor (pilot bore + 4 screws) and has a
# round lobe around the motor axis.  Right plate (normal +X) has 4 mounting
# holes.  Top and bottom gussets join them; the back-left side is cut on a
# diagonal and the inside is pocketed from the diagonal / left side.

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- driving dimensions (mm) ----------------
H = 60.0            # overall height (Z)
DEPTH = 75.0        # overall depth (Y)
BOX_W = 54.2        # width of the box part (X), right face at x = 0
BULGE_R = 31.7      # radius of the round lobe of the motor plate
LOBE_X = -34.1      # centre of the lobe (X); lobe centre Z = motor axis
MOT_X = -38.2       # motor axis X
MOT_Z = H / 2.0     # motor axis Z
T_FRONT = 9.3       # motor (front) plate thickness
T_RIGHT = 12.6      # mounting (right) plate thickness
T_TB = 5.5          # top / bottom gusset thickness
DIAG_Y0 = 24.7      # diagonal starts at (x=-BOX_W, y=DIAG_Y0)
DIAG_X1 = -14.3     # diagonal ends at (x=DIAG_X1, y=DEPTH)
RIM_BACK = 1.0      # rim left at the back end of the pocket

BORE_D = 19.6       # motor pilot bore
MOT_HOLE_D = 5.8    # motor screw holes
MOT_PCR = 15.0      # motor screw pitch radius

MNT_HOLE_D = 7.8    # mounting holes on the right face
MNT_Y = (18.75, 56.25)
MNT_Z = (15.9, H - 15.9)

R_OUT = 5.0         # outer round on the top/bottom edges of the left side
R_DIAG = 1.5        # small round on the top/bottom diagonal edges
R_CONCAVE = 0.8     # concave blend between plate outline and lobe
R_CORNER_V = 9.4    # inner fillet, vertical corner motor plate / right plate
R_RIGHT = 9.4       # inner fillets gussets / right plate
R_IN = 3.5          # inner fillets gussets / motor plate
R_BACK = 5.0        # inner fillets at the back end of the pocket
R_POCKET_RIM = 2.0  # round on the rim of the pocket opening
R_RIM = 2.0         # round on the back edge of the lobe
R_CLEAR_MOT = 8.0   # screw-head clearance (motor screw next to the corner)
R_CLEAR_MNT = 9.5   # screw-head clearance around the mounting holes
CLEAR_LEN = 11.0


def clip_poly(poly, a, b, c):
    """keep the part of a polygon where a*x + b*y <= c (Sutherland-Hodgman)"""
    out = []
    n = len(poly)
    for i in range(n):
        p = poly[i]
        q = poly[(i + 1) % n]
        fp = a * p[0] + b * p[1] - c
        fq = a * q[0] + b * q[1] - c
        if fp <= 0:
            out.append(p)
        if (fp < 0 < fq) or (fq < 0 < fp):
            t = fp / (fp - fq)
            out.append((p[0] + t * (q[0] - p[0]), p[1] + t * (q[1] - p[1])))
    return out


def arc_mid(center, r, p0, p1):
    a0 = math.atan2(p0[1] - center[1], p0[0] - center[0])
    a1 = math.atan2(p1[1] - center[1], p1[0] - center[0])
    da = (a1 - a0 + math.pi) % (2 * math.pi) - math.pi
    am = a0 + da / 2.0
    return (center[0] + r * math.cos(am), center[1] + r * math.sin(am))


def try_fillet(wp, edges, r):
    if not edges:
        return wp
    try:
        res = wp.newObject(edges).fillet(r)
        if res.val().isValid():
            return res
    except Exception:
        pass
    return wp


def multi_fillet(wp, pairs):
    """fillet several edges with individual radii in a single blend"""
    try:
        mk = BRepFilletAPI_MakeFillet(wp.val().wrapped)
        for r, e in pairs:
            mk.Add(r, e.wrapped)
        mk.Build()
        if mk.IsDone():
            res = cq.Shape.cast(mk.Shape())
            if res.isValid():
                return cq.Workplane("XY").newObject([res])
    except Exception:
        pass
    # fall back to the big rounds only
    return try_fillet(wp, [e for r, e in pairs if r == max(p[0] for p in pairs)],
                      max(p[0] for p in pairs))


# ---------------- motor plate lobe (outline in the XZ plane) ----------------
xl = -BOX_W
dxb = xl - R_CONCAVE - LOBE_X
dzb = math.sqrt((BULGE_R + R_CONCAVE) ** 2 - dxb ** 2)
zc_hi = MOT_Z + dzb
zc_lo = MOT_Z - dzb
cb_hi = (xl - R_CONCAVE, zc_hi)
cb_lo = (xl - R_CONCAVE, zc_lo)


def on_bulge(cb):
    vx, vz = cb[0] - LOBE_X, cb[1] - MOT_Z
    L = math.hypot(vx, vz)
    return (LOBE_X + BULGE_R * vx / L, MOT_Z + BULGE_R * vz / L)


t2_hi = on_bulge(cb_hi)
t2_lo = on_bulge(cb_lo)

lobe = (
    cq.Workplane("XZ")
    .moveTo(xl + 2.0, zc_hi)
    .lineTo(xl, zc_hi)
    .threePointArc(arc_mid(cb_hi, R_CONCAVE, (xl, zc_hi), t2_hi), t2_hi)
    .threePointArc((LOBE_X - BULGE_R, MOT_Z), t2_lo)
    .threePointArc(arc_mid(cb_lo, R_CONCAVE, t2_lo, (xl, zc_lo)), (xl, zc_lo))
    .lineTo(xl + 2.0, zc_lo)
    .close()
    .extrude(-T_FRONT)      # XZ normal is -Y -> negative extrude goes +Y
)

# ---------------- box body (plan pentagon, full height) ----------------
pent = [(-BOX_W, 0.0), (0.0, 0.0), (0.0, DEPTH), (DIAG_X1, DEPTH), (-BOX_W, DIAG_Y0)]
box = cq.Workplane("XY").polyline(pent).close().extrude(H)

dx, dy = DIAG_X1 - (-BOX_W), DEPTH - DIAG_Y0
dlen = math.hypot(dx, dy)
ux, uy = dx / dlen, dy / dlen           # along the diagonal
nx, ny = uy, -ux                        # inward normal of the diagonal face


def on_diag(m, tol=1e-3):
    return abs((m.x + BOX_W) * nx + (m.y - DIAG_Y0) * ny) < tol


# outer rounds: big round along the top/bottom edges of the left side and a
# small round along the top/bottom diagonal edges (one blend operation)
pairs = []
for e in box.val().Edges():
    m = e.Center()
    if not (abs(m.z - H) < 1e-3 or abs(m.z) < 1e-3):
        continue
    if abs(m.x + BOX_W) < 1e-3:
        pairs.append((R_OUT, e))
    elif on_diag(m):
        pairs.append((R_DIAG, e))
box = multi_fillet(box, pairs)

# round on the back edge of the lobe
sel = [e for e in lobe.edges().vals()
       if abs(e.Center().y - T_FRONT) < 1e-3 and e.Center().x < -BOX_W - 0.2]
lobe = try_fillet(lobe, sel, R_RIM)

body = box.union(lobe, clean=True)

# ---------------- pocket (open to the diagonal face and the left side) ----------------
u_max = dlen - RIM_BACK
BIG_X, BIG_Y = -80.0, 100.0
big = [(BIG_X, T_FRONT), (-T_RIGHT, T_FRONT), (-T_RIGHT, BIG_Y), (BIG_X, BIG_Y)]
c_lim = u_max + (-BOX_W) * ux + DIAG_Y0 * uy
pocket_pl = clip_poly(big, ux, uy, c_lim)
pocket = (
    cq.Workplane("XY").workplane(offset=T_TB)
    .polyline(pocket_pl).close()
    .extrude(H - 2 * T_TB)
)


def inner_edge(m):
    return m.x > BIG_X + 1.0 and m.y < BIG_Y - 1.0


def at_tb(m):
    return abs(m.z - T_TB) < 1e-3 or abs(m.z - (H - T_TB)) < 1e-3


# small fillets where the gussets meet the motor plate
sel = [e for e in pocket.edges().vals()
       if inner_edge(e.Center()) and at_tb(e.Center()) and abs(e.Center().y - T_FRONT) < 1e-3]
pocket = try_fillet(pocket, sel, R_IN)

# large fillets along the right (mounting) plate
sel = [e for e in pocket.edges().vals()
       if inner_edge(e.Center()) and at_tb(e.Center()) and abs(e.Center().x + T_RIGHT) < 1e-3]
pocket = try_fillet(pocket, sel, R_RIGHT)

# vertical corner motor plate / right plate (if not already rounded)
sel = [e for e in pocket.edges().vals()
       if abs(e.Center().x + T_RIGHT) < 1e-3 and abs(e.Center().y - T_FRONT) < 1e-3]
pocket = try_fillet(pocket, sel, R_CORNER_V)


# back end wall of the pocket
def on_back_wall(m):
    return inner_edge(m) and abs((m.x + BOX_W) * ux + (m.y - DIAG_Y0) * uy - u_max) < 1e-3


sel = [e for e in pocket.edges().vals() if on_back_wall(e.Center())]
pocket = try_fillet(pocket, sel, R_BACK)

body = body.cut(pocket)

# round the rim of the pocket opening on the diagonal face
sel = [e for e in body.edges().vals()
       if on_diag(e.Center(), 0.05) and T_TB - 0.6 < e.Center().z < H - T_TB + 0.6
       and -BOX_W + 0.5 < e.Center().x < DIAG_X1 - 0.3]
body = try_fillet(body, sel, R_POCKET_RIM)

# ---------------- screw-head clearance milled into the inner fillets ----------------
# only inside the pocket envelope (the plate faces themselves stay flat)
env = (
    cq.Workplane("XY").workplane(offset=T_TB)
    .polyline(pocket_pl).close()
    .extrude(H - 2 * T_TB)
)
mot_pts = []
for a in (0, 90, 180, 270):
    mot_pts.append((MOT_X + MOT_PCR * math.cos(math.radians(a)),
                    MOT_Z + MOT_PCR * math.sin(math.radians(a))))
clear = (cq.Workplane("XZ").workplane(offset=-T_FRONT)
         .center(mot_pts[0][0], mot_pts[0][1]).circle(R_CLEAR_MOT).extrude(-CLEAR_LEN))
for yy in MNT_Y:
    for zz in MNT_Z:
        c = (cq.Workplane("YZ").workplane(offset=-T_RIGHT)
             .center(yy, zz).circle(R_CLEAR_MNT).extrude(-CLEAR_LEN))
        clear = clear.union(c)
clear = clear.intersect(env)
body = body.cut(clear)

# ---------------- holes ----------------
body = body.cut(
    cq.Workplane("XZ").center(MOT_X, MOT_Z).circle(BORE_D / 2.0).extrude(-50)
)
for (hx, hz) in mot_pts:
    body = body.cut(
        cq.Workplane("XZ").center(hx, hz).circle(MOT_HOLE_D / 2.0).extrude(-50)
    )
for yy in MNT_Y:
    for zz in MNT_Z:
        body = body.cut(
            cq.Workplane("YZ").workplane(offset=-30).center(yy, zz)
            .circle(MNT_HOLE_D / 2.0).extrude(40)
        )

result = body
